import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Box-shaped servo actuator with a sheet-metal U-bracket on top.
# X = across the body (side horn axis), Y = body length, Z = height.
# ---------------------------------------------------------------------------

# ---- servo body ----
W = 36.4          # core housing width (X)
L = 50.0          # body length (Y)
H = 30.6          # body height (Z)
CH = 2.0          # chamfer of the +/-Y horizontal edges
PAD_T = 2.3       # thickness of the side pads (idler end)
PAD_Y1 = -13.0    # pad straight edge (= boss axis Y)
PAD_R = 8.3       # radius of the pad bulge around the boss
AXZ = H / 2.0     # height of the side axes
HORN_Y = 13.0     # output horn axis (Y)
BOSS_Y = -13.0    # idler boss axis (Y)
HORN_D = 21.8     # horn disk diameter
HORN_T = 2.0      # horn disk thickness
HORN_RING = 8.5   # horn hole circle radius
HUB_D = 8.3       # horn hub diameter
BOSS_D = 8.5      # idler boss diameter
BOSS_LEN = 6.4    # idler boss length beyond the pad
BOSS_FIL = 1.0    # fillet at the boss base
END_Y0 = 18.2     # start of the +Y corner pockets
POCKET_D = 2.8    # depth of the +Y corner screw pockets
POCKET_H = 7.0    # height of the +Y corner screw pockets
SIDE_X = 14.9     # inner edge of the corner pieces
CORNER_Y = -17.6  # end of the -Y corner pieces
EDGE_CH = 0.5     # small chamfer of the long top/bottom edges
SCREW_D = 3.2     # screw head diameter

# ---- bracket ----
T = 2.0                     # sheet thickness
BR_W = 26.4                 # bracket base width (X) incl. side lips
ARM_W = 21.8                # arm width (X)
BR_Y0 = -26.6               # outer face of the -Y arm
BR_Y1 = 17.9                # outer face of the +Y arm
BR_YC = (BR_Y0 + BR_Y1) / 2.0
ARM_H = 32.4                # arm height above the body top
AX_H = 29.75                # bracket axis height above the body top
NOTCH_R = 4.4               # U-notch radius in the arms
NOTCH_F = 1.6               # fillet at the notch lips
ARM_RC = 2.5                # arm top corner radius
R_IN, R_OUT = 0.3, 1.5      # bend radii
LIP_H = 5.3                 # side lip height
LIP_Y0, LIP_Y1 = -23.8, 15.2
SLOT_W, SLOT_H, SLOT_Z = 6.4, 9.9, 11.9
ARM_HOLE_R = 8.5
ARM_HOLE_D = 2.1

ZB = H              # bracket base bottom
ZAX = H + AX_H      # bracket axis height (world)
ZTOP = ZB + ARM_H   # arm top


# ------------------------------ helpers ------------------------------------
def cyl_x(d, x0, x1, y, z):
    lo, hi = min(x0, x1), max(x0, x1)
    return (cq.Workplane("YZ", origin=(lo, 0, 0)).center(y, z)
            .circle(d / 2.0).extrude(hi - lo))


def cyl_y(d, y0, y1, x, z):
    lo, hi = min(y0, y1), max(y0, y1)
    return (cq.Workplane("XZ", origin=(0, hi, 0)).center(x, z)
            .circle(d / 2.0).extrude(hi - lo))


def cyl_z(d, z0, z1, x, y):
    lo, hi = min(z0, z1), max(z0, z1)
    return (cq.Workplane("XY", origin=(0, 0, lo)).center(x, y)
            .circle(d / 2.0).extrude(hi - lo))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(abs(x1 - x0), abs(y1 - y0), abs(z1 - z0), centered=False)
            .translate((min(x0, x1), min(y0, y1), min(z0, z1))))


def arc_mid(c, r, a0, a1):
    am = 0.5 * (a0 + a1)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def phillips_x(s, x_face, y, z, depth=0.9):
    """screw on a +/-X face: returns (cut, add) solids"""
    cut = cyl_x(SCREW_D + 0.4, x_face, x_face - s * depth, y, z)
    cone = cq.Solid.makeCone((SCREW_D + 1.2) / 2.0, (SCREW_D + 0.4) / 2.0, 0.4,
                             cq.Vector(x_face + s * 0.001, y, z), cq.Vector(-s, 0, 0))
    cut = cut.union(cq.Workplane("XY").add(cone))
    head = cyl_x(SCREW_D, x_face - s * depth, x_face - s * 0.25, y, z)
    xr = x_face - s * 0.25
    cross = box(min(xr, xr - s * 0.6), max(xr, xr - s * 0.6),
                y - 1.1, y + 1.1, z - 0.25, z + 0.25)
    cross = cross.union(box(min(xr, xr - s * 0.6), max(xr, xr - s * 0.6),
                            y - 0.25, y + 0.25, z - 1.1, z + 1.1))
    return cut, head.cut(cross)


# ------------------------------ body ---------------------------------------
core = (cq.Workplane("XY").box(W, L, H, centered=(True, True, False))
        .edges("|X").chamfer(CH).edges("|Y").chamfer(EDGE_CH))

# envelope giving the side pieces the same end chamfers
env = (cq.Workplane("XY").box(W + 2 * PAD_T + 10, L, H, centered=(True, True, False))
       .edges("|X").chamfer(CH))

body = core
adds = []
for s in (1, -1):
    x_in = s * W / 2.0
    x_out = s * (W / 2.0 + PAD_T)
    # idler-end pad: rectangle + round bulge around the boss
    pad = (cq.Workplane("YZ", origin=(min(x_in, x_out), 0, 0))
           .center((-L / 2.0 + PAD_Y1) / 2.0, H / 2.0)
           .rect(PAD_Y1 + L / 2.0, H).extrude(PAD_T))
    pad = pad.union(cyl_x(2 * PAD_R, x_in, x_out, PAD_Y1, AXZ))
    for zj in (AXZ - PAD_R, AXZ + PAD_R):
        pad = pad.edges(cq.selectors.BoxSelector(
            (-50, PAD_Y1 - 0.05, zj - 0.05), (50, PAD_Y1 + 0.05, zj + 0.05))).fillet(1.0)
    pad = pad.intersect(env)
    pad = pad.faces(">X" if s > 0 else "<X").edges("|Z").edges(
        cq.selectors.BoxSelector((-50, -L / 2 - 0.1, -1), (50, -L / 2 + 0.1, H + 1))).chamfer(0.5)
    body = body.union(pad)

    # +Y end: screw pockets at the top and bottom corners, seam line between
    xa, xb = s * (W / 2.0 - POCKET_D), s * (W / 2.0 + 1.0)
    for zlo, zhi in ((-1.0, POCKET_H), (H - POCKET_H, H + 1.0)):
        body = body.cut(box(min(xa, xb), max(xa, xb), END_Y0, L / 2.0 + 1.0, zlo, zhi))
    xs0 = s * W / 2.0
    body = body.cut(box(xs0 - 0.15, xs0 + 0.15, END_Y0 - 0.15, END_Y0 + 0.15, -1, H + 1))
    # shallow window on the back face between the pockets
    body = body.cut(box(min(xa, xb), max(xa, xb), L / 2.0 - 0.7, L / 2.0 + 1.0,
                        POCKET_H, H - POCKET_H))

    # output horn disk
    horn = cyl_x(HORN_D, x_in, x_in + s * HORN_T, HORN_Y, AXZ)
    horn = horn.faces(">X" if s > 0 else "<X").edges().chamfer(0.4)
    body = body.union(horn)

    # idler boss with a fillet at its base
    boss = cyl_x(BOSS_D, x_out - s * 0.5, x_out + s * BOSS_LEN, BOSS_Y, AXZ)
    boss = boss.faces(">X" if s > 0 else "<X").edges().chamfer(0.4)
    rb, fb = BOSS_D / 2.0, BOSS_FIL
    ring = (cq.Workplane("XZ").moveTo(rb - 0.05, 0).lineTo(rb + fb, 0)
            .threePointArc((rb + fb * (1 - math.sqrt(0.5)), fb * (1 - math.sqrt(0.5))),
                           (rb, fb))
            .lineTo(rb - 0.05, fb).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    ring = ring.rotate((0, 0, 0), (0, 1, 0), 90 * s).translate((x_out, BOSS_Y, AXZ))
    body = body.union(boss).union(ring)

# -X side: thin stepped plate under the idler pad
SK_T = 0.5
sk_pts = [(-L / 2.0, H), (-8.6, H), (-8.6, AXZ + 11.0), (-3.9, AXZ + 6.0),
          (-3.9, AXZ - 6.0), (-8.6, AXZ - 11.0), (-8.6, 0.0), (-L / 2.0, 0.0)]
skirt = (cq.Workplane("YZ", origin=(-W / 2.0 - SK_T, 0, 0))
         .polyline(sk_pts).close().extrude(SK_T + 0.2)).intersect(env)
body = body.union(skirt)

# horn hub +X: plain raised cap
hub_p = cyl_x(HUB_D, W / 2 + HORN_T, W / 2 + HORN_T + 1.4, HORN_Y, AXZ)
hub_p = hub_p.faces(">X").edges().fillet(0.5)
body = body.union(hub_p)
# horn hub -X: recessed ring with splined hub
xf = -W / 2 - HORN_T
body = body.cut(cyl_x(11.0, xf, xf + 0.8, HORN_Y, AXZ))
hub_m = cyl_x(8.2, xf + 0.8, xf - 1.3, HORN_Y, AXZ).faces("<X").edges().chamfer(0.3)
body = body.union(hub_m)
body = body.cut(cyl_x(5.0, xf - 1.3, xf + 0.5, HORN_Y, AXZ))
body = body.union(box(xf - 0.9, xf + 0.6, HORN_Y - 0.8, HORN_Y + 0.8, AXZ - 1.7, AXZ + 1.7)
                  .intersect(cyl_x(5.0, xf - 0.9, xf + 0.6, HORN_Y, AXZ)))

# horn holes (8 on a ring), idler centre holes
for s in (1, -1):
    x_face = s * (W / 2.0 + HORN_T)
    for k in range(8):
        a = math.radians(45 * k)
        d = 2.3 if k % 2 == 0 else 1.8
        yy = HORN_Y + HORN_RING * math.cos(a)
        zz = AXZ + HORN_RING * math.sin(a)
        body = body.cut(cyl_x(d, x_face, x_face - s * 1.5, yy, zz))
    xb = s * (W / 2.0 + PAD_T + BOSS_LEN)
    body = body.cut(cyl_x(1.6, xb, xb - s * 3.0, BOSS_Y, AXZ))

# screws / holes on the sides
for s in (1, -1):
    xo = s * (W / 2.0 + PAD_T)
    xe = s * (W / 2.0 - POCKET_D)
    xc = s * W / 2.0
    for zz in (3.3, H - 3.3):
        # pad corners: phillips screws on +X, countersunk holes on -X
        if s > 0:
            c, a = phillips_x(s, xo, -L / 2 + 3.4, zz)
            body = body.cut(c)
            adds.append(a)
        else:
            body = body.cut(cyl_x(3.4, xo, xo - s * 0.6, -L / 2 + 3.4, zz))
            body = body.cut(cyl_x(2.6, xo, xo - s * 1.2, -L / 2 + 3.4, zz))
            body = body.cut(cyl_x(1.6, xo, xo - s * 4.0, -L / 2 + 3.4, zz))
        # +Y corner screws (on the pocket floors)
        c, a = phillips_x(s, xe, L / 2 - 3.6, zz)
        body = body.cut(c)
        adds.append(a)
        # plain holes beside the horn (+X side only)
        if s > 0:
            body = body.cut(cyl_x(2.2, xc, xc - s * 2.5, 4.4, zz))
    # screw under the horn (+X side only)
    if s > 0:
        c, a = phillips_x(s, xc, HORN_Y, 2.4, depth=0.7)
        body = body.cut(c)
        adds.append(a)

# front face holes (4) and back face holes (2)
for xx in (-6.3, 6.3):
    for zz in (AXZ - 8.6, AXZ + 8.6):
        body = body.cut(cyl_y(2.4, -L / 2.0, -L / 2.0 + 3.0, xx, zz))
for zz in (AXZ - 8.6, AXZ + 8.6):
    body = body.cut(cyl_y(2.4, L / 2.0, L / 2.0 - 3.0, 7.0, zz))

# bottom holes
for xx in (-8.4, 5.2):
    for yy in (-16.4, 10.5):
        body = body.cut(cyl_z(2.2, 0, 3.0, xx, yy))

# threaded holes in the top face under the bracket fixing holes
for xx in (-6.5, 6.5):
    for yy in (BR_YC - 13.0, BR_YC + 13.0):
        body = body.cut(cyl_z(2.0, H - 3.0, H + 0.1, xx, yy))

# connector sockets on top and bottom near the -X edge
CON_X, CON_Y = -14.9, -2.4          # socket centre
CON_W, CON_L = 3.3, 10.0            # socket opening
for z0, sgn in ((H, -1), (0.0, 1)):
    zlo = min(z0, z0 + sgn * 1.5)
    sock = (cq.Workplane("XY", origin=(0, 0, zlo)).center(CON_X, CON_Y)
            .rect(CON_W, CON_L).extrude(1.5).edges("|Z").fillet(0.6))
    body = body.cut(sock)
    zp = min(z0 + sgn * 1.5, z0 + sgn * 0.4)
    plug = (cq.Workplane("XY", origin=(0, 0, zp)).center(CON_X, CON_Y)
            .rect(1.6, CON_L - 1.8).extrude(1.1))
    body = body.union(plug)
    # connector housing outline (parting lines)
    zg0, zg1 = (H - 0.25, H + 0.1) if sgn < 0 else (-0.1, 0.25)
    for yy in (CON_Y + CON_L / 2 + 0.6, CON_Y - CON_L / 2 - 0.6):
        body = body.cut(box(-W / 2 - 0.1, CON_X + CON_W / 2 + 0.2, yy - 0.12, yy + 0.12, zg0, zg1))

# seam grooves (housing parting lines)
G = 0.25
for s in (1, -1):
    xs = s * W / 2.0
    # pad / core seam on the front face
    body = body.cut(box(xs - G / 2, xs + G / 2, -L / 2 - 0.1, -L / 2 + G, -1, H + 1))
    # corner-piece outlines on top and bottom faces (-Y end)
    xg = s * SIDE_X
    for zlo, zhi in ((H - G, H + 0.1), (-0.1, G)):
        body = body.cut(box(xg - G / 2, xg + G / 2, -L / 2, CORNER_Y, zlo, zhi))
        body = body.cut(box(min(xg, xs), max(xg, xs), CORNER_Y - G / 2, CORNER_Y + G / 2,
                            zlo, zhi))
    # corner tabs on the front face
    for yf, sg in ((-L / 2, 1),):
        for zt, zb in ((H - CH - 0.2, H - 7.4), (CH + 0.2, 7.4)):
            zl, zh = min(zt, zb), max(zt, zb)
            body = body.cut(box(xg - G / 2, xg + G / 2, yf - 0.1 * sg, yf + G * sg,
                                zl, zh))
            body = body.cut(box(min(xg, xs), max(xg, xs), yf - 0.1 * sg, yf + G * sg,
                                zb - G / 2, zb + G / 2))
# back face: short parting groove at the +X end
body = body.cut(box(13.7, W / 2 + 1.0, L / 2 - 0.3, L / 2 + 0.1, AXZ - 0.15, AXZ + 0.15))

# vertical seam on the side faces between horn and pad
xs = -W / 2.0
SEAM_Y = 2.6
body = body.cut(box(xs - G, xs + G, SEAM_Y - 0.3, SEAM_Y + 0.3, -1, H + 1))

for a in adds:
    body = body.union(a)

# ------------------------------ bracket ------------------------------------
# U profile (YZ) : base + both arms with bends, extruded across the arm width
zt_u = ZB + T + 6.0
y0, y1, z0 = BR_Y0, BR_Y1, ZB
ri, ro = R_IN, R_OUT
c1 = (y0 + ro, z0 + ro)
c2 = (y1 - ro, z0 + ro)
c3 = (y1 - T - ri, z0 + T + ri)
c4 = (y0 + T + ri, z0 + T + ri)
u = (cq.Workplane("YZ", origin=(-ARM_W / 2.0, 0, 0))
     .moveTo(y0, zt_u)
     .lineTo(y0, z0 + ro)
     .threePointArc(arc_mid(c1, ro, math.pi, 1.5 * math.pi), (y0 + ro, z0))
     .lineTo(y1 - ro, z0)
     .threePointArc(arc_mid(c2, ro, 1.5 * math.pi, 2 * math.pi), (y1, z0 + ro))
     .lineTo(y1, zt_u)
     .lineTo(y1 - T, zt_u)
     .lineTo(y1 - T, z0 + T + ri)
     .threePointArc(arc_mid(c3, ri, 0, -0.5 * math.pi), (y1 - T - ri, z0 + T))
     .lineTo(y0 + T + ri, z0 + T)
     .threePointArc(arc_mid(c4, ri, -0.5 * math.pi, -math.pi), (y0 + T, z0 + T + ri))
     .lineTo(y0 + T, zt_u)
     .close()
     .extrude(ARM_W))
bracket = u

# arm outline (XZ) with rounded top corners and a filleted U notch
a_ = ARM_W / 2.0
zc = ZAX
dz = ZTOP - NOTCH_F - zc
xfc = math.sqrt((NOTCH_R + NOTCH_F) ** 2 - dz ** 2)       # fillet centre x
k = NOTCH_R / (NOTCH_R + NOTCH_F)
tpx, tpz = xfc * k, zc + dz * k                           # tangent point on notch
aL = math.atan2(tpz - (ZTOP - NOTCH_F), xfc - tpx)        # angle seen from left fillet centre
z_arm0 = ZB + T + 3.0


def arm_solid(y_hi):
    w = (cq.Workplane("XZ", origin=(0, y_hi, 0))
         .moveTo(-a_, z_arm0)
         .lineTo(-a_, ZTOP - ARM_RC)
         .threePointArc(arc_mid((-a_ + ARM_RC, ZTOP - ARM_RC), ARM_RC, math.pi, 0.5 * math.pi),
                        (-a_ + ARM_RC, ZTOP))
         .lineTo(-xfc, ZTOP)
         .threePointArc(arc_mid((-xfc, ZTOP - NOTCH_F), NOTCH_F, 0.5 * math.pi, aL),
                        (-tpx, tpz))
         .threePointArc((0, zc - NOTCH_R), (tpx, tpz))
         .threePointArc(arc_mid((xfc, ZTOP - NOTCH_F), NOTCH_F, math.pi - aL, 0.5 * math.pi),
                        (xfc, ZTOP))
         .lineTo(a_ - ARM_RC, ZTOP)
         .threePointArc(arc_mid((a_ - ARM_RC, ZTOP - ARM_RC), ARM_RC, 0.5 * math.pi, 0.0),
                        (a_, ZTOP - ARM_RC))
         .lineTo(a_, z_arm0)
         .close()
         .extrude(T))
    return w


bracket = bracket.union(arm_solid(BR_Y0 + T)).union(arm_solid(BR_Y1))

# side lips (XZ profile with bend) extruded along Y
for s in (1, -1):
    xo = BR_W / 2.0
    xs_ = ARM_W / 2.0 - 1.0
    cl1 = (xo - ro, z0 + ro)
    cl2 = (xo - T - ri, z0 + T + ri)
    lip = (cq.Workplane("XZ", origin=(0, LIP_Y1, 0))
           .moveTo(xs_, z0)
           .lineTo(xo - ro, z0)
           .threePointArc(arc_mid(cl1, ro, -0.5 * math.pi, 0.0), (xo, z0 + ro))
           .lineTo(xo, z0 + LIP_H)
           .lineTo(xo - T, z0 + LIP_H)
           .lineTo(xo - T, z0 + T + ri)
           .threePointArc(arc_mid(cl2, ri, 0.0, -0.5 * math.pi), (xo - T - ri, z0 + T))
           .lineTo(xs_, z0 + T)
           .close()
           .extrude(LIP_Y1 - LIP_Y0))
    lip = lip.edges("|X").edges(">Z").fillet(1.5)
    if s < 0:
        lip = lip.mirror("YZ")
    bracket = bracket.union(lip)

# base plate holes
bracket = bracket.cut(cyl_z(8.8, ZB - 1, ZB + T + 1, 0, BR_YC))
for kk in range(8):
    a = math.radians(45 * kk)
    bracket = bracket.cut(cyl_z(2.1, ZB - 1, ZB + T + 1,
                                8.5 * math.cos(a), BR_YC + 8.5 * math.sin(a)))
for kk in range(4):
    for off, d in ((23.5, 2.1), (67.0, 2.8)):
        a = math.radians(off + 90 * kk)
        bracket = bracket.cut(cyl_z(d, ZB - 1, ZB + T + 1,
                                    9.35 * math.cos(a), BR_YC + 9.35 * math.sin(a)))
for xx in (-6.5, 6.5):
    for yy in (BR_YC - 13.0, BR_YC + 13.0):
        bracket = bracket.cut(cyl_z(2.8, ZB - 1, ZB + T + 1, xx, yy))

# arm holes and slots
for ang in (0, 180, 225, 270, 315):
    a = math.radians(ang)
    bracket = bracket.cut(cyl_y(ARM_HOLE_D, BR_Y0 - 1, BR_Y1 + 1,
                                ARM_HOLE_R * math.cos(a), ZAX + ARM_HOLE_R * math.sin(a)))
slot = (cq.Workplane("XZ", origin=(0, BR_Y1 + 1, 0)).center(0, ZB + SLOT_Z)
        .rect(SLOT_W, SLOT_H).extrude(BR_Y1 - BR_Y0 + 2).edges("|Y").fillet(1.0))
bracket = bracket.cut(slot)

# idler bearing on the inner side of the -Y arm
yi = BR_Y0 + T
bearing = cyl_y(20.9, yi, yi + 2.2, 0, ZAX)
bearing = bearing.faces(">Y").edges().chamfer(0.3)
bearing = bearing.union(cyl_y(11.8, yi + 2.2, yi + 8.0, 0, ZAX))
bearing = bearing.union(cyl_y(11.0, yi + 8.0, yi + 8.6, 0, ZAX))
capb = cyl_y(11.8, yi + 8.6, yi + 9.8, 0, ZAX).faces(">Y").edges().fillet(0.8)
bearing = bearing.union(capb)
bearing = bearing.cut(cyl_y(8.6, yi - 0.1, yi + 5.5, 0, ZAX))
bearing = bearing.union(cyl_y(6.4, yi + 4.8, yi + 5.5, 0, ZAX))
bearing = bearing.cut(cyl_y(2.6, yi - 0.1, yi + 10.0, 0, ZAX))
bearing = bearing.cut(cyl_y(12.6, yi - 0.1, yi + 0.3, 0, ZAX)
                      .cut(cyl_y(12.0, yi - 0.2, yi + 0.4, 0, ZAX)))
for kk in range(8):
    a = math.radians(45 * kk)
    bearing = bearing.cut(cyl_y(1.8, yi - 0.1, yi + 2.3,
                                8.5 * math.cos(a), ZAX + 8.5 * math.sin(a)))

# output horn on the inner side of the +Y arm
yo = BR_Y1 - T
bhorn = cyl_y(20.9, yo - 2.3, yo, 0, ZAX)
bhorn = bhorn.faces("<Y").edges().chamfer(0.4)
bhorn = bhorn.union(cyl_y(8.4, yo - 2.9, yo + T + 0.7, 0, ZAX))
bhorn = bhorn.cut(cyl_y(6.4, yo - 3.0, yo - 2.6, 0, ZAX))
bhorn = bhorn.cut(cyl_y(5.0, yo - 3.0, yo - 0.4, 0, ZAX))
for kk in range(16):
    tooth = (box(-0.3, 0.3, yo - 3.0, yo - 0.4, ZAX + 2.2, ZAX + 2.9)
             .rotate((0, 0, ZAX), (0, 1, ZAX), 360.0 / 16 * kk))
    bhorn = bhorn.cut(tooth)
bhorn = bhorn.cut(cyl_y(2.4, yo - 3.0, yo + T + 1.0, 0, ZAX))
for kk in range(8):
    a = math.radians(45 * kk)
    bhorn = bhorn.cut(cyl_y(1.8, yo - 2.4, yo + 0.1,
                            8.5 * math.cos(a), ZAX + 8.5 * math.sin(a)))

bracket = bracket.union(bearing).union(bhorn)

result = body.union(bracket)

VIEW = {"azimuth": 45, "elevation": 26}
